import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 57.0          # body length (X)
W = 29.5          # body width (Y)
H = 11.3          # body height (Z)
C_CORNER = 2.25   # vertical corner chamfer of body

T_RIM = 3.0       # rim wall thickness
D_LEDGE = 2.4     # depth of ledge (first step) below top
D_FLOOR = 5.2     # depth of deep floor below top
LEDGE_W = 2.8     # ledge width around deep pocket (left / sides)
LEDGE_W_R = 2.7   # ledge width at +X end of deep pocket
W_POCKET = 17.0   # width (Y) of deep pocket
W_NOTCH = 16.5    # width (Y) of the notch through the +X wall (ledge depth)
R_POCKET = 0.8    # vertical corner rounds inside pockets
R_NOTCH = 0.7     # rounds on the outer mouth of the +X notch

# deep pocket widening that reaches the side walls
X_EXT0 = -4.4     # start of widening (x)
X_EXT1 = 13.4     # end of widening (x)
EXT_CHAMFER = 3.4 # 45 deg chamfer on +Y side at start of widening

# boss with countersunk hole
BOSS_X = -7.9
BOSS_Y = -1.7
BOSS_R = 5.6
BOSS_TOP = H - D_LEDGE - 0.2
BOSS_FILLET = 1.0
BOSS_HOLE_D = 5.2
BOSS_CB_D = 6.9       # counterbore diameter at boss top
BOSS_CB_DEPTH = 4.0   # counterbore depth (cylindrical part)
BOSS_CB_ANGLE = 60.0  # included angle of conical transition

# mounting ears
EAR_R = 7.5
EAR_OFF = 7.4     # distance from body side face to ear centre
EAR_H = 6.0
EAR_PLAN_FILLET = 7.0
EAR_TOP_FILLET = 1.2
EAR_HOLE_D = 6.75
EAR_CSK_D = 8.35
EAR_BOT_CHAMFER = 0.6

# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .box(L, W, H, centered=(True, True, False))
    .edges("|Z")
    .chamfer(C_CORNER)
)


# ---------------- ears ----------------
def ear_plate(sign):
    yb = W / 2.0
    yc = yb + EAR_OFF
    rf = EAR_PLAN_FILLET
    R = EAR_R
    xf = math.sqrt((R + rf) ** 2 - (rf - EAR_OFF) ** 2)
    F = (xf, yb + rf)
    dx, dy = 0 - F[0], yc - F[1]
    dl = math.hypot(dx, dy)
    T1 = (F[0] + rf * dx / dl, F[1] + rf * dy / dl)
    # mid point of fillet arc
    a0 = math.atan2(yb - F[1], xf - F[0])
    a1 = math.atan2(T1[1] - F[1], T1[0] - F[0])
    if a1 - a0 > math.pi:
        a1 -= 2 * math.pi
    elif a0 - a1 > math.pi:
        a1 += 2 * math.pi
    am = 0.5 * (a0 + a1)
    M1 = (F[0] + rf * math.cos(am), F[1] + rf * math.sin(am))
    s = sign
    pts = lambda p: (p[0], s * p[1])
    wp = (
        cq.Workplane("XY")
        .moveTo(*pts((xf, yb - 2.0)))
        .lineTo(*pts((xf, yb)))
        .threePointArc(pts(M1), pts(T1))
        .threePointArc(pts((0.0, yc + R)), pts((-T1[0], T1[1])))
        .threePointArc(pts((-M1[0], M1[1])), pts((-xf, yb)))
        .lineTo(*pts((-xf, yb - 2.0)))
        .close()
        .extrude(EAR_H)
    )
    return wp


part = body.union(ear_plate(1)).union(ear_plate(-1))

# fillet between ear top and body side wall
for s in (1, -1):
    part = part.edges(
        cq.selectors.BoxSelector(
            (-3.0, s * W / 2.0 - 0.1, EAR_H - 0.1), (3.0, s * W / 2.0 + 0.1, EAR_H + 0.1)
        )
    ).fillet(EAR_TOP_FILLET)

# ---------------- ledge pocket (first step) ----------------
xi = L / 2.0 - T_RIM
yi = W / 2.0 - T_RIM
ledge = cq.Workplane("XY").workplane(offset=H - D_LEDGE).center(0, 0).rect(2 * xi, 2 * yi).extrude(D_LEDGE + 1)
notch = (
    cq.Workplane("XY")
    .workplane(offset=H - D_LEDGE)
    .center((xi + L / 2.0 + 2.0) / 2.0, 0)
    .rect(L / 2.0 + 2.0 - xi + 1.0, W_NOTCH)
    .extrude(D_LEDGE + 1)
)
part = part.cut(ledge).cut(notch)

# ---------------- deep pocket ----------------
xa = -xi + LEDGE_W
xb = xi - LEDGE_W_R
hp = W_POCKET / 2.0
deep_pts = [
    (xa, -hp),
    (X_EXT0, -hp),
    (X_EXT0, -yi),
    (X_EXT1, -yi),
    (X_EXT1, -hp),
    (xb, -hp),
    (xb, hp),
    (X_EXT1, hp),
    (X_EXT1, yi),
    (X_EXT0 + EXT_CHAMFER, yi),
    (X_EXT0, hp),
    (xa, hp),
]
deep = (
    cq.Workplane("XY")
    .workplane(offset=H - D_FLOOR)
    .polyline(deep_pts)
    .close()
    .extrude(D_FLOOR + 1)
)
part = part.cut(deep)


# vertical corner rounds inside the pockets / notch
def round_vertical(wp, pts, r, tol=0.05):
    sel = []
    for e in wp.val().Edges():
        if e.geomType() != "LINE":
            continue
        p0 = e.startPoint()
        p1 = e.endPoint()
        if abs(p0.x - p1.x) > 1e-4 or abs(p0.y - p1.y) > 1e-4:
            continue
        for (x, y) in pts:
            if abs(p0.x - x) < tol and abs(p0.y - y) < tol:
                sel.append(e)
                break
    return wp.newObject(sel).fillet(r)


round_pts = [
    (xa, -hp), (xa, hp), (xb, -hp), (xb, hp),          # deep pocket corners
    (X_EXT0, -hp), (X_EXT1, -hp), (X_EXT1, hp),        # ledge convex corners
    (X_EXT0, hp),                                      # chamfer start
    (xi, -W_NOTCH / 2.0), (xi, W_NOTCH / 2.0),         # notch stubs
]
part = round_vertical(part, round_pts, R_POCKET)
part = round_vertical(part, [(L / 2.0, -W_NOTCH / 2.0), (L / 2.0, W_NOTCH / 2.0)], R_NOTCH)

# ---------------- boss ----------------
boss = (
    cq.Workplane("XY")
    .workplane(offset=H - D_FLOOR - 0.5)
    .center(BOSS_X, BOSS_Y)
    .circle(BOSS_R)
    .extrude(BOSS_TOP - (H - D_FLOOR - 0.5))
)
part = part.union(boss)

# boss base fillet
part = part.edges(
    cq.selectors.BoxSelector(
        (BOSS_X - BOSS_R - 0.2, BOSS_Y - BOSS_R - 0.2, H - D_FLOOR - 0.1),
        (BOSS_X + BOSS_R + 0.2, BOSS_Y + BOSS_R + 0.2, H - D_FLOOR + 0.1),
    )
).fillet(BOSS_FILLET)

# boss hole: counterbore from top with conical transition to through hole
r_cb = BOSS_CB_D / 2.0
r_h = BOSS_HOLE_D / 2.0
cone_h = (r_cb - r_h) / math.tan(math.radians(BOSS_CB_ANGLE / 2.0))
z_cb = BOSS_TOP - BOSS_CB_DEPTH
bh = cq.Solid.makeCylinder(r_h, BOSS_TOP + 2.0, cq.Vector(BOSS_X, BOSS_Y, -1.0))
bcb = cq.Solid.makeCylinder(r_cb, BOSS_CB_DEPTH + 1.0, cq.Vector(BOSS_X, BOSS_Y, z_cb))
bcone = cq.Solid.makeCone(r_h, r_cb, cone_h, cq.Vector(BOSS_X, BOSS_Y, z_cb - cone_h))
part = part.cut(cq.Workplane().add(bh)).cut(cq.Workplane().add(bcb)).cut(cq.Workplane().add(bcone))

# ear holes: through, countersunk on top, chamfered on bottom
for s in (1, -1):
    yc = s * (W / 2.0 + EAR_OFF)
    hole = (
        cq.Workplane("XY").workplane(offset=-1).center(0, yc)
        .circle(EAR_HOLE_D / 2.0).extrude(EAR_H + 2)
    )
    csk_h = (EAR_CSK_D - EAR_HOLE_D) / 2.0
    csk = cq.Solid.makeCone(EAR_HOLE_D / 2.0, EAR_CSK_D / 2.0 + 1.0, csk_h + 1.0,
                            cq.Vector(0, yc, EAR_H - csk_h), cq.Vector(0, 0, 1))
    bot = cq.Solid.makeCone(EAR_HOLE_D / 2.0 + EAR_BOT_CHAMFER + 1.0, EAR_HOLE_D / 2.0,
                            EAR_BOT_CHAMFER + 1.0, cq.Vector(0, yc, -1.0), cq.Vector(0, 0, 1))
    part = part.cut(hole).cut(cq.Workplane().add(csk)).cut(cq.Workplane().add(bot))

result = part
